import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FW = 32.0          # frame outer width (X)
FL = 32.0          # frame outer length (Y)
FH = 7.2           # frame height (Z)
WALL = 1.45        # frame wall thickness
WALL_B = 1.7       # rear wall thickness (slightly heavier, carries the clip)
CORNER_R = 1.3     # outer vertical corner radius
BOT_R = 1.35       # outer bottom edge fillet
FLOOR_T = 1.4      # floor strip thickness
OPEN_HW = 7.0      # half width of the central opening between the floor strips

HOLE_D = 3.2       # floor strip holes
HOLE_X = 10.0
HOLE_Y = 10.0
SLOT_X0 = 8.85     # floor slot inner edge (abs X)
SLOT_X1 = 12.8     # floor slot outer edge (abs X)
SLOT_HL = 6.9      # floor slot half length (Y)
SLOT_R = 1.9       # rounded inner corners of floor slot

PLATE_T = 1.85     # hanging plate thickness
PLATE_Y0 = -7.1    # hanging plate Y extent (front end, both plates)
PLATE_Y1_P = 7.95  # rear end of the +X plate
PLATE_Y1_N = 7.1   # rear end of the -X plate
PLATE_DEPTH = 7.9  # below frame bottom
PLATE_R = 3.9      # bottom corner radius

EAR_T = 2.7        # ear / tab / cap thickness (top flush with frame top)
EAR_HW = 3.95      # front ear half width
EAR_IN = 12.8      # front ear inner edge (abs Y)
EAR_HOLE_D = 2.6
Z0 = FH - EAR_T    # underside of ears / tab
FRONT_CUT_TOP = Z0 # front wall cut-out top
BACK_CUT_TOP = 3.35# back wall cut-out top
CUT_R = 1.4

TAB_HW = 3.92      # rear tab half width
TAB_IN = 13.1      # rear tab inner edge (Y)
TAB_HOLE_Y = 15.15
NECK_HW = 3.5

CYL_Y = 25.0       # clip axis position (Y)
CYL_R = 7.37       # clip outer radius
CYL_BOT = -9.7     # clip bottom Z
CAP_R = 6.65       # radius of the shallow top recesses
CAP_TAB_DEG = 30.0 # angular width of the full-radius lands at the top
REC_Z = 5.3        # bottom of the vertical recess face
REC_Z2 = 4.3       # recess bevel meets the outer surface
CAP_HOLE_D = 3.7   # counterbore in the cap
CAP_HOLE_D2 = 2.4  # through hole into the socket
SOCK_R = 5.6       # socket bore radius (domed top)
SOCK_Z = -6.0      # centre of the socket dome (Z)
SLOT_W = 3.7       # clip slot width
SLOT_TOP = 0.2     # clip slot top Z
BOT_CH = 0.8       # bottom outer chamfer

WEB_HW = 3.95      # web blocks under the rear tab
WEB_Z0 = 2.66

# ---------------- frame ----------------
outer = (
    cq.Workplane("XY")
    .rect(FW, FL)
    .extrude(FH)
    .edges("|Z").fillet(CORNER_R)
    .faces("<Z").edges().fillet(BOT_R)
)
inner_w = FW - 2 * WALL
inner_l = FL - WALL - WALL_B
inner_cy = (WALL - WALL_B) / 2
pocket = (
    cq.Workplane("XY", origin=(0, inner_cy, FLOOR_T))
    .rect(inner_w, inner_l)
    .extrude(FH)
    .edges("|Z").fillet(0.3)
)
frame = outer.cut(pocket)
# central opening through the floor
opening = cq.Workplane("XY", origin=(0, inner_cy, -1)).rect(2 * OPEN_HW, inner_l).extrude(FH + 2)
frame = frame.cut(opening)


def wall_cut(y_face, top):
    # U shaped cut-out in a front/back wall, open at the bottom, rounded top corners
    h = top + 1.0
    blk = (
        cq.Workplane("XZ")
        .center(0, top - h / 2)
        .rect(2 * OPEN_HW, h)
        .extrude(-WALL * 3, both=True)
        .translate((0, y_face, 0))
    )
    return blk.edges("|Y").edges(">Z").fillet(CUT_R)


frame = frame.cut(wall_cut(-FL / 2, FRONT_CUT_TOP))
frame = frame.cut(wall_cut(FL / 2, BACK_CUT_TOP))

# floor holes
for sx in (-1, 1):
    for sy in (-1, 1):
        frame = frame.cut(
            cq.Workplane("XY", origin=(sx * HOLE_X, sy * HOLE_Y, -1)).circle(HOLE_D / 2).extrude(FLOOR_T + 2)
        )


def floor_slot(sx):
    w = SLOT_X1 - SLOT_X0
    cx = sx * (SLOT_X0 + SLOT_X1) / 2
    s = cq.Workplane("XY", origin=(cx, 0, -1)).rect(w, 2 * SLOT_HL).extrude(FLOOR_T + 2)
    # round the two corners on the inner side (toward the centre)
    sel = "<X" if sx > 0 else ">X"
    return s.edges("|Z").edges(sel).fillet(SLOT_R)


for sx in (-1, 1):
    frame = frame.cut(floor_slot(sx))

# hanging plates under the floor strips
for sx, y1 in ((-1, PLATE_Y1_N), (1, PLATE_Y1_P)):
    x0 = sx * (OPEN_HW + PLATE_T / 2)
    plate = (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .center((PLATE_Y0 + y1) / 2, -PLATE_DEPTH / 2 + 0.5)
        .rect(y1 - PLATE_Y0, PLATE_DEPTH + 1.0)
        .extrude(PLATE_T / 2, both=True)
    )
    plate = plate.edges("|X").edges("<Z").fillet(PLATE_R)
    frame = frame.union(plate)

# ---------------- front ear ----------------
ear = (
    cq.Workplane("XY", origin=(0, 0, Z0))
    .moveTo(-EAR_HW, -EAR_IN)
    .lineTo(EAR_HW, -EAR_IN)
    .lineTo(EAR_HW, -FL / 2)
    .threePointArc((0, -FL / 2 - EAR_HW), (-EAR_HW, -FL / 2))
    .close()
    .extrude(EAR_T)
)
ear = ear.edges("|Z").edges(">Y").fillet(0.9)

# ---------------- rear tab, neck, web ----------------
tab = (
    cq.Workplane("XY", origin=(0, 0, Z0))
    .center(0, (TAB_IN + FL / 2 + 0.5) / 2)
    .rect(2 * TAB_HW, FL / 2 + 0.5 - TAB_IN)
    .extrude(EAR_T)
)
tab = tab.edges("|Z").edges("<Y").fillet(0.7)
neck = (
    cq.Workplane("XY", origin=(0, 0, Z0))
    .center(0, (FL / 2 + CYL_Y) / 2)
    .rect(2 * NECK_HW, CYL_Y - FL / 2)
    .extrude(EAR_T)
)
web_y0 = FL / 2 - WALL_B
web = (
    cq.Workplane("XY", origin=(0, 0, WEB_Z0))
    .center(0, (web_y0 + CYL_Y) / 2)
    .rect(2 * WEB_HW, CYL_Y - web_y0)
    .extrude(Z0 - WEB_Z0 + 0.01)
)

# ---------------- clip cylinder (ball socket with four fingers) ----------------
body = (
    cq.Workplane("XY", origin=(0, CYL_Y, CYL_BOT))
    .circle(CYL_R)
    .extrude(FH - CYL_BOT)
    .faces("<Z").edges().chamfer(BOT_CH)
)
# shallow recesses in the four diagonal quadrants at the top of the cylinder:
# vertical face at CAP_R down to REC_Z, then a steep bevel out to the full radius
span = 90.0 - CAP_TAB_DEG
slope = (REC_Z - REC_Z2) / (CYL_R - CAP_R)
ro = CYL_R + 1.0
rec_profile = (
    cq.Workplane("XZ")
    .polyline([
        (CAP_R, FH + 1.0),
        (CAP_R, REC_Z),
        (ro, REC_Z - slope * (ro - CAP_R)),
        (ro, FH + 1.0),
    ])
    .close()
    .revolve(span, (0, 0, 0), (0, 1, 0))
)
for k in range(4):
    rec = rec_profile.rotate((0, 0, 0), (0, 0, 1), CAP_TAB_DEG / 2 + 90.0 * k).translate((0, CYL_Y, 0))
    body = body.cut(rec)

clip = body.union(neck).union(tab).union(web)
# socket: bore open at the bottom with a domed (spherical) top
c45 = math.cos(math.radians(45.0))
socket = (
    cq.Workplane("XZ")
    .moveTo(0, CYL_BOT - 1.0)
    .lineTo(SOCK_R, CYL_BOT - 1.0)
    .lineTo(SOCK_R, SOCK_Z)
    .threePointArc((SOCK_R * c45, SOCK_Z + SOCK_R * c45), (0, SOCK_Z + SOCK_R))
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((0, CYL_Y, 0))
)
clip = clip.cut(socket)
# vertical slots (open at the bottom) forming four flexible fingers
for w, l in ((2 * CYL_R + 4, SLOT_W), (SLOT_W, 2 * CYL_R + 4)):
    cutter = (
        cq.Workplane("XY", origin=(0, CYL_Y, CYL_BOT - 1))
        .rect(w, l)
        .extrude(SLOT_TOP - CYL_BOT + 1)
    )
    clip = clip.cut(cutter)

result = frame.union(ear).union(clip)

# holes (cut last so they pass through everything below them)
result = result.cut(cq.Workplane("XY", origin=(0, -FL / 2, -2)).circle(EAR_HOLE_D / 2).extrude(FH + 4))
result = result.cut(cq.Workplane("XY", origin=(0, TAB_HOLE_Y, -2)).circle(EAR_HOLE_D / 2).extrude(FH + 4))
result = result.cut(
    cq.Workplane("XY", origin=(0, CYL_Y, Z0)).circle(CAP_HOLE_D / 2).extrude(EAR_T + 1)
)
result = result.cut(
    cq.Workplane("XY", origin=(0, CYL_Y, SOCK_Z)).circle(CAP_HOLE_D2 / 2).extrude(FH - SOCK_Z + 1)
)

VIEW = {"azimuth": 45, "elevation": 26}
